import cadquery as cq
import math

# HC-SR04 style ultrasonic sensor module.
# X = board length, Y = board width, Z up; board top face at z = 0.

# ---------------- driving dimensions (mm) ----------------
PCB_L, PCB_W, PCB_T = 45.0, 20.0, 1.8          # printed circuit board
HOLE_D, HOLE_INSET = 1.0, 1.0                  # 4 corner mounting holes
PAD_D, PAD_T = 1.9, 0.05                       # copper ring around each hole

TR_DX = 12.45          # transducer centre offset from board centre (x)
TR_D = 16.0            # transducer can diameter
TR_H = 12.05           # can height above board (inner rim edge)
RIM_DROP = 0.25        # rim top slopes down towards the outer edge
BORE_D = 12.9          # top opening diameter
BORE_DEPTH = 5.5       # depth of the annular well around the centre boss
BOSS_D = 8.4           # centre (radiator) boss diameter
BOSS_TOP = 2.1         # boss top below can top
CONE_DEPTH = 2.6       # depth of the conical dish (at the centre hole)
CTR_HOLE_D = 1.4       # small hole at the cone apex
CTR_HOLE_DEPTH = 0.8

XT_L, XT_W, XT_H = 10.0, 3.4, 2.7              # HC-49/S crystal (stadium outline)
XT_Y = -7.2
XT_FIL = 0.3
XT_BASE_L, XT_BASE_W, XT_BASE_T = 11.0, 4.15, 0.06

TXT = "HC-SR04"                                # silkscreen legend
TXT_SIZE, TXT_T, TXT_Y = 2.1, 0.04, -4.1

HDR_PITCH, HDR_N = 2.54, 4                     # 4-pin header on the under side
HDR_Y0, HDR_Y1 = 7.7, 10.0
HDR_H = 2.5
PIN_W = 0.55                                   # round pins
PIN_Y = 8.88
PIN_TOP = 0.78                                 # solder stub above board
PIN_BELOW = 6.1                                # pin length below the header body

LEAD_W, LEAD_L, LEAD_T, LEAD_P = 0.42, 1.05, 0.28, 1.27
# (x, y, body length along x, body width along y, height, pins per side, leads on the +/-x sides?)
ICS = [
    (18.37, 1.15, 3.95, 10.4, 1.87, 8, True),     # SOIC-16, long axis along Y
    (-17.4, -0.4, 8.65, 3.9, 1.92, 7, False),  # SOIC-14, long axis along X
    (0.3, -1.1, 8.65, 3.9, 1.75, 7, False),    # SOIC-14, long axis along X
]

# ---------------- board ----------------
board = cq.Workplane("XY").box(PCB_L, PCB_W, PCB_T, centered=(True, True, False)).translate((0, 0, -PCB_T))
hole_pts = [(sx * (PCB_L / 2 - HOLE_INSET), sy * (PCB_W / 2 - HOLE_INSET)) for sx in (-1, 1) for sy in (-1, 1)]
pads_top = cq.Workplane("XY").pushPoints(hole_pts).circle(PAD_D / 2).extrude(PAD_T)
pads_bot = (cq.Workplane("XY").workplane(offset=-PCB_T - PAD_T).pushPoints(hole_pts)
            .circle(PAD_D / 2).extrude(PAD_T))
board = board.union(pads_top).union(pads_bot)
board = board.cut(cq.Workplane("XY").workplane(offset=-PCB_T - 1).pushPoints(hole_pts)
                  .circle(HOLE_D / 2).extrude(PCB_T + 2))


# ---------------- transducers ----------------
def transducer():
    """Can with a top well, a raised centre boss and a conical dish (revolved profile)."""
    r0, rb, rc = TR_D / 2, BORE_D / 2, BOSS_D / 2
    h = TR_H
    rh = CTR_HOLE_D / 2
    zc = h - BOSS_TOP - CONE_DEPTH
    pts = [
        (0, 0),
        (r0, 0),
        (r0, h - RIM_DROP),
        (rb, h),
        (rb, h - BORE_DEPTH),
        (rc, h - BORE_DEPTH),
        (rc, h - BOSS_TOP),
        (rh, zc),
        (rh, zc - CTR_HOLE_DEPTH),
        (0, zc - CTR_HOLE_DEPTH),
    ]
    prof = cq.Workplane("XZ").polyline(pts).close()
    # seam turned onto the silhouette of the default view
    return prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), 45)


can = transducer()
cans = can.translate((-TR_DX, 0, 0)).union(can.translate((TR_DX, 0, 0)))


# ---------------- crystal ----------------
def stadium(L, W, H):
    return cq.Workplane("XY").slot2D(L, W).extrude(H)


xtal = stadium(XT_L, XT_W, XT_H).faces(">Z").edges().fillet(XT_FIL)
xtal = xtal.union(stadium(XT_BASE_L, XT_BASE_W, XT_BASE_T)).translate((0, XT_Y, 0))

# ---------------- header + pins ----------------
hdr_len = HDR_PITCH * HDR_N
hdr_w = HDR_Y1 - HDR_Y0
pin_x = [(i - (HDR_N - 1) / 2) * HDR_PITCH for i in range(HDR_N)]
header = (cq.Workplane("XY").box(hdr_len, hdr_w, HDR_H - 0.3, centered=(True, False, False))
          .translate((0, HDR_Y0, -PCB_T - HDR_H + 0.3)))
# small stand-off feet under each pin position
feet = (cq.Workplane("XY").workplane(offset=-PCB_T - HDR_H)
        .pushPoints([(x, HDR_Y0 + hdr_w / 2) for x in pin_x])
        .rect(HDR_PITCH - 0.35, hdr_w).extrude(0.31))
header = header.union(feet)
# shallow grooves between pin cells on the long faces
for i in range(1, HDR_N):
    gx = (i - HDR_N / 2) * HDR_PITCH
    for gy in (HDR_Y0, HDR_Y1):
        header = header.cut(cq.Workplane("XY").box(0.25, 0.3, HDR_H, centered=(True, True, False))
                            .translate((gx, gy, -PCB_T - HDR_H)))

pin_len = PCB_T + HDR_H + PIN_BELOW + 0.2
pins = (cq.Workplane("XY").workplane(offset=-PCB_T - HDR_H - PIN_BELOW)
        .pushPoints([(x, PIN_Y) for x in pin_x]).circle(PIN_W / 2).extrude(pin_len))
# rounded solder stubs on the top side, with a solder bridge between the two +x pins
stubs = (cq.Workplane("XY").pushPoints([(x, PIN_Y) for x in pin_x])
         .circle(0.3).extrude(PIN_TOP).faces(">Z").edges().fillet(0.18))
bridge = (cq.Workplane("XY").center((pin_x[2] + pin_x[3]) / 2, PIN_Y)
          .slot2D(pin_x[3] - pin_x[2] + 0.5, 0.45).extrude(0.25))
pins = pins.union(stubs).union(bridge)


# ---------------- SOIC packages on the under side ----------------
def soic(x, y, lx, wy, hz, n, along_y):
    z0 = -PCB_T
    body = (cq.Workplane("XY").box(lx, wy, hz, centered=(True, True, False))
            .edges("|Z").chamfer(0.12)
            .translate((x, y, z0 - hz)))
    # gull-wing leads simplified: a foot flat against the board plus a shoulder on the body side
    span = (n - 1) * LEAD_P
    feet, shoulders = [], []
    if along_y:
        for k in range(n):
            yy = y - span / 2 + k * LEAD_P
            for s in (-1, 1):
                feet.append((x + s * (lx / 2 + LEAD_L / 2 - 0.2), yy, LEAD_L + 0.4, LEAD_W))
                shoulders.append((x + s * (lx / 2 + 0.15), yy, 0.5, LEAD_W))
    else:
        for k in range(n):
            xx = x - span / 2 + k * LEAD_P
            for s in (-1, 1):
                feet.append((xx, y + s * (wy / 2 + LEAD_L / 2 - 0.2), LEAD_W, LEAD_L + 0.4))
                shoulders.append((xx, y + s * (wy / 2 + 0.15), LEAD_W, 0.5))
    for (px, py, ax, ay) in feet:
        body = body.union(cq.Workplane("XY").box(ax, ay, LEAD_T, centered=(True, True, False))
                          .translate((px, py, z0 - LEAD_T)))
    for (px, py, ax, ay) in shoulders:
        body = body.union(cq.Workplane("XY").box(ax, ay, 0.45, centered=(True, True, False))
                          .translate((px, py, z0 - 0.45)))
    return body


ics = None
for spec in ICS:
    b = soic(*spec)
    ics = b if ics is None else ics.union(b)

# ---------------- small passives (0603 size) on the under side ----------------
SMD_L, SMD_W, SMD_H = 1.55, 0.8, 0.5           # component body
SMD_CAP_L, SMD_CAP_H = 0.35, 0.58              # metallised end caps (slightly proud)
PAD_ONLY_T = 0.25                              # bare footprints: pad height
# (x, y, axis of the part, fitted?)  -- unfitted footprints show only their two pads
SMD = [
    (-0.2, -7.85, "x", 1), (-6.05, -7.05, "x", 0), (-12.4, -7.6, "x", 1), (-8.1, -4.5, "y", 0),
    (-10.9, -4.4, "y", 0), (-9.1, -1.4, "x", 0), (-11.2, -1.0, "y", 0), (-12.0, 2.4, "x", 0),
    (-7.5, 2.3, "y", 0), (-8.2, 5.8, "x", 0), (-10.6, 5.4, "y", 0), (-10.6, 8.5, "x", 0),
    (-4.0, 4.5, "x", 1), (-0.8, 6.05, "x", 1), (-18.6, 8.2, "x", 1), (-21.3, 5.6, "y", 1),
    (7.4, -8.95, "x", 1), (7.1, -3.9, "x", 1), (6.35, 0.5, "x", 1), (17.1, -6.3, "x", 1),
    (12.05, -2.25, "y", 1), (12.0, 1.25, "y", 1), (9.5, 4.5, "x", 1), (3.5, 6.3, "x", 1),
    (-19.2, -7.7, "y", 1), (-16.3, -7.75, "x", 1), (-21.1, -5.1, "y", 1), (-16.75, -4.85, "x", 1),
    (-13.0, -7.75, "y", 1), (-14.9, -3.8, "y", 1), (-15.5, 5.0, "x", 1), (-15.0, 8.3, "y", 1),
    (-5.05, -9.35, "x", 0),
]


def _blk(cx, cy, lx, ly, h):
    return (cq.Workplane("XY").box(lx, ly, h, centered=(True, True, False))
            .translate((cx, cy, -PCB_T - h)))


smd = None
for (sx_, sy_, ax_, fitted) in SMD:
    along_x = ax_ == "x"
    off = (SMD_L - SMD_CAP_L) / 2
    ends = [(sx_ + s_ * off, sy_) if along_x else (sx_, sy_ + s_ * off) for s_ in (-1, 1)]
    if fitted:
        part = _blk(sx_, sy_, SMD_L if along_x else SMD_W, SMD_W if along_x else SMD_L, SMD_H)
        for (ex, ey) in ends:
            part = part.union(_blk(ex, ey, SMD_CAP_L if along_x else SMD_W + 0.06,
                                   SMD_W + 0.06 if along_x else SMD_CAP_L, SMD_CAP_H))
    else:
        part = None
        for (ex, ey) in ends:
            p = _blk(ex, ey, 0.7 if along_x else 0.8, 0.8 if along_x else 0.7, PAD_ONLY_T)
            part = p if part is None else part.union(p)
    smd = part if smd is None else smd.union(part)

result = board.union(cans).union(xtal).union(header).union(pins).union(ics).union(smd)

# ---------------- silkscreen legend (upside down, reads from the back edge) ----------------
try:
    legend = (cq.Workplane("XY").text(TXT, TXT_SIZE, TXT_T, halign="center", valign="center")
              .rotate((0, 0, 0), (0, 0, 1), 180).translate((0, TXT_Y, 0)))
    result = result.union(legend)
except Exception:
    pass
